import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 153.0          # outer length along X
D = 97.2           # outer depth along Y
H = 69.6           # outer height along Z
T = 1.4            # wall thickness
T_FLOOR = 1.4      # floor thickness

# cable slot in the left (-X) wall, open at the top
SLOT_W = 7.0
SLOT_DEPTH = 19.5
SLOT_Y = -D / 2 + 0.32 * D     # slot centre along Y

# PCB standoff bosses on the floor (x, y) relative to box centre
BOSS_OD = 5.4
BOSS_H = 5.0
BOSS_HOLE = 2.5
BOSS_HOLE_DEPTH = 4.5
BOSS_DX = 0.15     # small global shift of the boss pattern along X
BOSSES = [
    (-21.0 + BOSS_DX, 26.3),
    (43.0 + BOSS_DX, 26.3),
    (-8.6 + BOSS_DX, -2.0),
    (64.6 + BOSS_DX, -2.0),
    (-8.6 + BOSS_DX, -37.5),
    (64.6 + BOSS_DX, -37.5),
]

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- open-top box ----------------
outer = cq.Workplane("XY").box(L, D, H, centered=(True, True, False))
cavity = (
    cq.Workplane("XY")
    .workplane(offset=T_FLOOR)
    .box(L - 2 * T, D - 2 * T, H, centered=(True, True, False))
)
body = outer.cut(cavity)

# ---------------- slot in the -X wall ----------------
slot = (
    cq.Workplane("XY")
    .workplane(offset=H - SLOT_DEPTH)
    .center(-L / 2 + T / 2, SLOT_Y)
    .box(T * 4, SLOT_W, SLOT_DEPTH + 1.0, centered=(True, True, False))
)
body = body.cut(slot)

# ---------------- standoff bosses ----------------
bosses = (
    cq.Workplane("XY")
    .workplane(offset=T_FLOOR)
    .pushPoints(BOSSES)
    .circle(BOSS_OD / 2)
    .extrude(BOSS_H)
)
body = body.union(bosses)

holes = (
    cq.Workplane("XY")
    .workplane(offset=T_FLOOR + BOSS_H - BOSS_HOLE_DEPTH)
    .pushPoints(BOSSES)
    .circle(BOSS_HOLE / 2)
    .extrude(BOSS_HOLE_DEPTH + 1.0)
)
body = body.cut(holes)

result = body
